import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 23.3            # width  (X)
H = 18.3            # height (Z)
D = 10.0            # thickness (Y) = length of the threaded hole
HOLE_Z = 2.5        # hole axis above the block centre
MAJOR = 12.0        # thread major diameter
PITCH = D / 6.0     # thread pitch (six full turns through the nut)
LEFT_HAND = False   # thread hand
THREAD_PHASE = 90.0 # rotation of the thread start about the hole axis (deg);
                    # 90 puts the crest at the top of the hole on the front face

# ISO 60 deg basic profile
H_FUND = PITCH * math.sqrt(3.0) / 2.0     # fundamental triangle height
DEPTH = 5.0 / 8.0 * H_FUND                # thread depth (major - minor)/2
MINOR = MAJOR - 2.0 * DEPTH               # minor diameter = bore
ROOT_FLAT = PITCH / 8.0                   # flat at the major diameter

VIEW = {"azimuth": 45, "elevation": 26}


def helical_groove(profile, pitch, length, left=False):
    """Helical cutting tool whose axial cross-section is the polygon
    `profile` [(r, z), ...]; axis +Z, starting at z=0 and running `length`.
    Built from ruled surfaces between coaxial helices (one per vertex)."""
    helices = []
    for r, z in profile:
        w = cq.Wire.makeHelix(pitch=pitch, height=length, radius=r,
                              center=cq.Vector(0, 0, z), lefthand=left)
        helices.append(w.Edges()[0])
    n = len(helices)
    faces = [cq.Face.makeRuledSurface(helices[i], helices[(i + 1) % n])
             for i in range(n)]
    for t in (0.0, 1.0):
        pts = [e.positionAt(t) for e in helices]
        faces.append(cq.Face.makeFromWires(cq.Wire.makePolygon(pts, close=True)))
    return cq.Solid.makeSolid(cq.Shell.makeShell(faces))


# ---------------- threaded block ----------------
r_bore = MINOR / 2.0
r_out = MAJOR / 2.0
tan30 = math.tan(math.radians(30.0))
hw_out = ROOT_FLAT / 2.0
tool_len = D + 2.0 * PITCH


def threaded_block(tool_dip, fuzzy):
    """Box with a tapped hole: a helical V-groove is cut first, then the bore
    at the minor diameter. `tool_dip` is how far the groove tool reaches
    inside the bore."""
    r_in = r_bore - tool_dip
    hw_in = hw_out + (r_out - r_in) * tan30
    profile = [(r_in, -hw_in), (r_out, -hw_out), (r_out, hw_out), (r_in, hw_in)]
    groove = (
        cq.Workplane()
        .add(helical_groove(profile, PITCH, tool_len, LEFT_HAND))
        .translate((0, 0, -tool_len / 2.0))
        .rotate((0, 0, 0), (0, 0, 1), THREAD_PHASE)
        .rotate((0, 0, 0), (1, 0, 0), -90)       # hole axis along Y
        .translate((0, 0, HOLE_Z))
    )
    bore = (
        cq.Workplane("XZ", origin=(0, D / 2.0, HOLE_Z))
        .circle(r_bore)
        .extrude(D)
    )
    blk = cq.Workplane("XY").box(W, D, H)
    return blk.cut(groove, tol=fuzzy).cut(bore, tol=fuzzy)


# expected volume (Pappus) to verify that the helical booleans succeeded
groove_area = 0.5 * (0.75 * PITCH + ROOT_FLAT) * DEPTH
groove_rc = r_bore + DEPTH * (0.75 * PITCH + 2 * ROOT_FLAT) / (3 * (0.75 * PITCH + ROOT_FLAT))
expected = W * D * H - math.pi * r_bore ** 2 * D \
    - groove_area * 2 * math.pi * groove_rc * D / PITCH

result = None
for dip, fz in ((0.15, 1e-4), (0.15, None), (0.2, 1e-4), (0.05, None), (0.12, 1e-4)):
    try:
        cand = threaded_block(dip, fz)
        sol = cand.val()
        if sol.isValid() and abs(sol.Volume() - expected) < 0.01 * expected:
            result = cand
            break
    except Exception:
        pass

if result is None:   # fallback: plain bore at the thread's pitch diameter
    plain = (
        cq.Workplane("XZ", origin=(0, D / 2.0, HOLE_Z))
        .circle(0.5 * (MAJOR - 0.65 * PITCH))
        .extrude(D)
    )
    result = cq.Workplane("XY").box(W, D, H).cut(plain)
